import math
import cadquery as cq

# ---------------------------------------------------------------
# Twin-plate arm with a worm-wheel style gear clamped between
# the round ends of two identical plates.
# Units: mm.  Plates lie in XY, arm runs along +Y, stack along +Z.
# Gear axis = Z axis through the origin.
# ---------------------------------------------------------------

# --- plate outline -------------------------------------------------
DISC_R = 27.2            # round end of each plate (gear axis at origin)
TIP_C = (31.1, 199.5)    # centre of the rounded far end
TIP_R = 8.75             # radius of the rounded far end
RIGHT_X = TIP_C[0] + TIP_R   # straight outer edge of the jaw
TIP_LEFT_ANG = 138.0     # where the outer (left) edge leaves the tip arc
HOOK_R = 3.2             # rounded tip of the hook under the jaw
HOOK_BOTTOM = (RIGHT_X - HOOK_R, 123.15)
JUNCTION_FILLET = 1.5    # arm meets round end

# outer (left) edge of the arm, from the tip down to the round end
LEFT_EDGE = [(17.4, 196.1), (8.2, 181.1), (1.3, 166.1), (-3.0, 152.0),
             (-6.4, 139.5), (-9.9, 120.0), (-13.15, 100.8), (-14.95, 81.5),
             (-16.0, 62.3), (-16.65, 43.0), (-16.95, 23.8), (-17.0, 8.0)]
# inner (right) edge of the arm, up over the notch to the hook bottom
RIGHT_EDGE = [(17.3, 8.0), (17.3, 30.0), (17.25, 50.0), (17.55, 75.0),
              (19.0, 100.8), (20.5, 111.2), (22.0, 120.2), (22.9, 124.5),
              (24.6, 128.5), (27.0, 129.75), (29.5, 128.7), (33.2, 125.3),
              HOOK_BOTTOM]

# --- stack heights ---------------------------------------------------
PLATE_T = 5.5
HUB_H = 3.2
HUB_R = 18.7
GEAR_H = 17.5

# --- gear (worm wheel) ----------------------------------------------
N_TEETH = 32
ROOT_RAD = 24.6
TIP_RAD = 28.05          # tooth tip radius at the gear faces
THROAT_RAD = 27.45       # tooth tip radius at mid height (worm throat)
TOOTH_W_ROOT = 3.1       # tooth width at the root
TOOTH_W_TOP = 2.6        # tooth width just below the blunt tip
TWIST_DEG = 3.0          # lead of the worm wheel teeth over the face width

# --- holes -----------------------------------------------------------
BORE_D = 8.2
BOLT_D = 5.2
BOLT_PCR = 13.7
CSK_D = 10.5
ARM_HOLES = [((0.0, 83.5), 7.4), ((31.1, 148.0), 7.2), ((31.1, 199.5), 7.2)]

Z_BOT_PLATE = 0.0
Z_HUB = Z_BOT_PLATE + PLATE_T
Z_GEAR = Z_HUB + HUB_H
Z_TOP_PLATE = Z_GEAR + GEAR_H
TOTAL_H = Z_TOP_PLATE + PLATE_T


def _pt_on_tip(ang_deg):
    a = math.radians(ang_deg)
    return (TIP_C[0] + TIP_R * math.cos(a), TIP_C[1] + TIP_R * math.sin(a))


def plate_solid(z0):
    a_left = math.radians(TIP_LEFT_ANG)
    p_left = _pt_on_tip(TIP_LEFT_ANG)
    p_mid = _pt_on_tip(TIP_LEFT_ANG / 2.0)
    t_left = (-math.sin(a_left), math.cos(a_left))

    hc = (HOOK_BOTTOM[0], HOOK_BOTTOM[1] + HOOK_R)       # hook arc centre
    hook_mid = (hc[0] + HOOK_R * math.cos(math.radians(-45)),
                hc[1] + HOOK_R * math.sin(math.radians(-45)))
    hook_top = (RIGHT_X, hc[1])

    arm = (
        cq.Workplane("XY").workplane(offset=z0)
        .moveTo(*RIGHT_EDGE[0])
        .spline(RIGHT_EDGE[1:], tangents=[(0.0, 1.0), (1.0, 0.0)], includeCurrent=True)
        .threePointArc(hook_mid, hook_top)
        .lineTo(RIGHT_X, TIP_C[1])
        .threePointArc(p_mid, p_left)
        .spline(LEFT_EDGE, tangents=[t_left, (0.0, -1.0)], includeCurrent=True)
        .close()
        .extrude(PLATE_T)
    )
    disc = cq.Workplane("XY").workplane(offset=z0).circle(DISC_R).extrude(PLATE_T)
    body = disc.union(arm)

    zc = z0 + PLATE_T / 2.0

    def vsel(x, y, d=1.5):
        return cq.selectors.BoxSelector((x - d, y - d, zc - 1), (x + d, y + d, zc + 1))

    # small fillets where the arm meets the round end
    xl = LEFT_EDGE[-2][0]
    xr = RIGHT_EDGE[1][0]
    yl = math.sqrt(DISC_R ** 2 - xl ** 2)
    yr = math.sqrt(DISC_R ** 2 - xr ** 2)
    body = body.edges(vsel(xl, yl)).fillet(JUNCTION_FILLET)
    body = body.edges(vsel(xr, yr)).fillet(JUNCTION_FILLET)

    # arm holes
    for (x, y), d in ARM_HOLES:
        body = body.cut(
            cq.Workplane("XY").workplane(offset=z0 - 1).center(x, y)
            .circle(d / 2).extrude(PLATE_T + 2)
        )
    return body


def tooth_section(z, apex_r, rot_deg):
    """Closed tooth profile at height z: one smooth spline from root to root
    over a blunt tip whose crest lies at radius apex_r."""
    r0 = ROOT_RAD - 0.4                # sink the tooth into the root cylinder
    hr = TOOTH_W_ROOT / 2.0
    ht = TOOTH_W_TOP / 2.0
    pts = [(r0, -hr),
           (apex_r - 0.9, -ht),
           (apex_r - 0.12, -0.62 * ht),
           (apex_r, 0.0),
           (apex_r - 0.12, 0.62 * ht),
           (apex_r - 0.9, ht),
           (r0, hr)]
    wire = (
        cq.Workplane("XY").workplane(offset=z)
        .moveTo(*pts[0])
        .spline(pts[1:], tangents=[(1.0, 0.08), (-1.0, 0.08)], includeCurrent=True)
        .close()
        .wires().val()
    )
    return wire.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), rot_deg)


def gear_solid():
    gear = cq.Workplane("XY").workplane(offset=Z_GEAR).circle(ROOT_RAD).extrude(GEAR_H)
    # one worm-wheel tooth: lofted through face / throat / face sections,
    # slightly twisted (worm lead) and shorter at mid height (throat)
    tooth = cq.Solid.makeLoft(
        [tooth_section(Z_GEAR, TIP_RAD, 0.0),
         tooth_section(Z_GEAR + GEAR_H / 2, THROAT_RAD, TWIST_DEG / 2),
         tooth_section(Z_GEAR + GEAR_H, TIP_RAD, TWIST_DEG)],
        False,
    )
    step = 360.0 / N_TEETH
    for i in range(N_TEETH):
        gear = gear.union(
            cq.Workplane("XY").add(tooth.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), i * step))
        )
    hub = cq.Workplane("XY").workplane(offset=Z_HUB).circle(HUB_R).extrude(HUB_H + 0.01)
    return gear.union(hub)


bottom = plate_solid(Z_BOT_PLATE)
top = plate_solid(Z_TOP_PLATE)
gear = gear_solid()

result = bottom.union(gear).union(top)

# through bore and bolt holes across the whole stack
result = result.cut(
    cq.Workplane("XY").workplane(offset=-1).circle(BORE_D / 2).extrude(TOTAL_H + 2)
)
bolt_pts = [(BOLT_PCR, 0), (-BOLT_PCR, 0), (0, BOLT_PCR), (0, -BOLT_PCR)]
result = result.cut(
    cq.Workplane("XY").workplane(offset=-1).pushPoints(bolt_pts)
    .circle(BOLT_D / 2).extrude(TOTAL_H + 2)
)
# 90 degree countersinks on the underside of the bottom plate
csk_depth = (CSK_D - BOLT_D) / 2.0
for (x, y) in bolt_pts:
    cone = cq.Solid.makeCone(CSK_D / 2 + 0.5, BOLT_D / 2 - 0.01, csk_depth + 0.5,
                             pnt=cq.Vector(x, y, Z_BOT_PLATE - 0.5), dir=cq.Vector(0, 0, 1))
    result = result.cut(cq.Workplane().add(cone))

VIEW = {"azimuth": 45, "elevation": 26}
